import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Desktop 6-axis robot arm: round base with turntable, shoulder bracket with
# servo, curved upper arm, forearm with roll sleeve, wrist and a geared
# parallel gripper.  Units: mm, Z up.
#
# The arm is built in its own frame (x' = joint-axis direction, the arm leans
# toward +y') and then yawed about Z by ARM_YAW on the turntable.
# ---------------------------------------------------------------------------

# ---- base ----
FLANGE_R = 52.0
FLANGE_T = 4.0
FLANGE_HOLE_R = 46.5
FLANGE_HOLE_D = 4.0
BODY_R = 43.0
BODY_WALL = 3.0
BODY_TOP = 49.0
CAP_R = 44.0
CAP_Z0 = 50.0
CAP_T = 4.0
CAP_TOP = CAP_Z0 + CAP_T
SIDE_HOLE_D = 7.0
SIDE_HOLE_Z = 13.0

# ---- arm pose (arm frame: (y', z)) ----
ARM_YAW = 11.0                # turntable rotation (deg, clockwise from top)
SHOULDER = (14.0, 83.0)
ELBOW = (41.0, 185.0)
WRIST = (89.0, 276.0)
GRIP_TILT = 25.4              # gripper axis tilt from vertical (toward +y')

# ---- shoulder bracket ----
BR_FACE = -5.5                # x' of the bracket face toward the upper arm
BR_T = 6.0
BR_RIM = 4.0
BR_DEPTH = 12.0
BR_ARC_R = 25.0
BR_Y0, BR_Y1 = -31.0, 23.5    # bracket foot on the turntable (y')
BR_LEAN = 12.0                # bracket lean about y' (top toward +x')
BR_EXTRA_YAW = 10.0           # extra yaw of the bracket about the shoulder

# ---- upper arm ----
UA_X0, UA_X1 = -2.5, 16.5     # x' extent of the link
UA_HALF_W = 15.5              # half width of the link (in plane)
UA_FILLET = 9.0               # edge rounding of the link
SHOULDER_HUB_R = 17.5
ELBOW_HUB_R = 16.5
UPPER_BOW = 2.5               # bow of the upper arm toward -y'
UA_TWIST = -15.0              # roll of the upper arm about its own axis

# ---- forearm ----
FORE_W = 33.0
FORE_OFF = 3.0                # forearm offset toward +y' (local)
FA_X0, FA_X1 = -19.0, 7.0     # x' extent of the forearm body
FA_BACK = -20.0               # x' of the elbow side plate back face

# ---- gripper ----
GX = -4.0                     # gripper centre x'
GEAR_R = 12.0
GEAR_DX = 14.75
GEAR_Z = 39.0
GEAR_Y = -9.5                 # gear layer (front)
JAW_T = 10.0


def tilt_of(p0, p1):
    """Angle (deg) from vertical of segment p0->p1 in the y'-z plane."""
    return math.degrees(math.atan2(p1[0] - p0[0], p1[1] - p0[1]))


def place(shape, tilt_deg, origin_yz, x=0.0):
    """Local frame: axis along +Z; rotate so +Z leans toward +Y by tilt."""
    return shape.rotate((0, 0, 0), (1, 0, 0), -tilt_deg).translate(
        (x, origin_yz[0], origin_yz[1]))


def lbox(sx, sy, sz, cx=0.0, cy=0.0, cz=0.0):
    return cq.Workplane("XY").box(sx, sy, sz).translate((cx, cy, cz))


def xcyl(r, x0, x1, y, z):
    """Cylinder along X from x0 to x1 centred at (y, z)."""
    return (cq.Workplane("YZ").workplane(offset=x0).center(y, z).circle(r)
            .extrude(x1 - x0))


def safe_fillet(wp, sel, r):
    """Fillet the selected edges; retry with a smaller radius if needed."""
    for rr in (r, 0.5 * r):
        try:
            res = wp.edges(sel).fillet(rr)
            if res.val().isValid():
                return res
        except Exception:
            pass
    return wp


# =========================== BASE ==========================================
flange = (cq.Workplane("XY").circle(FLANGE_R).circle(BODY_R - BODY_WALL)
          .extrude(FLANGE_T))
flange = flange.faces(">Z").workplane().polarArray(FLANGE_HOLE_R, 45, 360, 4) \
    .hole(FLANGE_HOLE_D)

body = (cq.Workplane("XY").workplane(offset=FLANGE_T)
        .circle(BODY_R).circle(BODY_R - BODY_WALL)
        .extrude(BODY_TOP - FLANGE_T))
neck = (cq.Workplane("XY").workplane(offset=BODY_TOP)
        .circle(BODY_R - 1.0).circle(BODY_R - BODY_WALL)
        .extrude(CAP_Z0 - BODY_TOP))
cap = (cq.Workplane("XY").workplane(offset=CAP_Z0).circle(CAP_R)
       .extrude(CAP_T))
cap = safe_fillet(cap, ">Z", 0.8)
base = flange.union(body).union(neck).union(cap)

# side hole on +X
base = base.cut(xcyl(SIDE_HOLE_D / 2, BODY_R - 6, BODY_R + 4, 0, SIDE_HOLE_Z))

# shallow vertical cable grooves on the front-right
for ang, wdt in ((-42.5, 6.0), (-55.5, 3.0), (-75.0, 0.8)):
    g = lbox(2.0, wdt, BODY_TOP - FLANGE_T - 2, BODY_R, 0,
             (BODY_TOP + FLANGE_T) / 2 + 1).rotate((0, 0, 0), (0, 0, 1), ang)
    base = base.cut(g)

# servo hanging under the turntable (seen from below)
US_ANG = -160.0               # azimuth of the base servo inside the base
US_R = 27.0
under_servo = lbox(16, 30, 32).rotate((0, 0, 0), (0, 0, 1), US_ANG).translate(
    (US_R * math.cos(math.radians(US_ANG)),
     US_R * math.sin(math.radians(US_ANG)), CAP_Z0 - 16))
usx = US_R * math.cos(math.radians(US_ANG))
usy = US_R * math.sin(math.radians(US_ANG))
hx, hy, hz = 9.0, 9.0, 16.0           # turntable horn (under side)
pl_ang = math.degrees(math.atan2(hy - usy, hx - usx))
pl_len = math.hypot(hx - usx, hy - usy)
under_plate = (cq.Workplane("XY").workplane(offset=hz + 2)
               .center(0.5 * (usx + hx), 0.5 * (usy + hy))
               .slot2D(pl_len + 16, 16, pl_ang).extrude(3))
under_horn = (cq.Workplane("XY").workplane(offset=hz)
              .center(hx, hy).slot2D(24, 9, 30).extrude(2.5))
under_horn = under_horn.union(under_plate).union(
    cq.Workplane("XY").workplane(offset=hz).center(hx, hy)
    .circle(4.0).extrude(CAP_Z0 - hz))
base = base.union(under_servo).union(under_horn)

# =========================== SHOULDER (arm frame) ==========================
SH_Y, SH_Z = SHOULDER


def bracket_outline(wp):
    cy, cz, r = SH_Y, SH_Z, BR_ARC_R
    px, pz = BR_Y0, CAP_TOP - 4
    dx, dz = cy - px, cz - pz
    dd = math.hypot(dx, dz)
    a = math.atan2(dz, dx) + math.asin(r / dd)      # upper tangent line
    tx = cy - r * math.sin(a)
    tz = cz + r * math.cos(a)
    rz = cz + math.sqrt(max(r * r - (BR_Y1 - cy) ** 2, 0.0))
    return (wp.moveTo(BR_Y0, CAP_TOP - 4).lineTo(BR_Y1, CAP_TOP - 4)
            .lineTo(BR_Y1, rz).threePointArc((cy, cz + r), (tx, tz)).close())


br_plate = bracket_outline(cq.Workplane("YZ").workplane(offset=BR_FACE)) \
    .extrude(-BR_T)
br_rim = bracket_outline(cq.Workplane("YZ")
                         .workplane(offset=BR_FACE - BR_T)).extrude(-BR_DEPTH)
br_rim = br_rim.cut(bracket_outline(cq.Workplane("YZ")
                                    .workplane(offset=BR_FACE - BR_T))
                    .offset2D(-BR_RIM).extrude(-BR_DEPTH))
bracket = br_plate.union(br_rim)
bracket = safe_fillet(bracket, "|X", 1.0)

SV_LEN = 31.0                  # servo body length along the shoulder axis
sh_servo = lbox(SV_LEN, 36, 16).rotate((0, 0, 0), (1, 0, 0), -45)
sh_servo = safe_fillet(sh_servo, "|X", 1.0).translate(
    (BR_FACE - BR_T - SV_LEN / 2, SH_Y - 7.0, SH_Z - 2.0))
sh_horn = xcyl(8.0, BR_FACE - 0.5, UA_X0 + 0.5, SH_Y, SH_Z)
shoulder = bracket.union(sh_servo).union(sh_horn)
# screw boss on the bracket face
shoulder = shoulder.union(xcyl(2.2, BR_FACE - 1.0, BR_FACE + 1.0,
                               SH_Y - 14, SH_Z - 12))
shoulder = shoulder.rotate((BR_FACE, 0, SH_Z), (BR_FACE, 1, SH_Z), BR_LEAN)
shoulder = shoulder.rotate((BR_FACE, SH_Y, 0), (BR_FACE, SH_Y, 1),
                           -BR_EXTRA_YAW)

# =========================== UPPER ARM (arm frame) =========================


def upper_link():
    sy, sz = SHOULDER
    ey, ez = ELBOW
    dy, dz = ey - sy, ez - sz
    L = math.hypot(dy, dz)
    ty, tz = dy / L, dz / L
    ny, nz = -tz, ty                  # left normal (toward -Y)
    my, mz = (sy + ey) / 2 + ny * UPPER_BOW, (sz + ez) / 2 + nz * UPPER_BOW
    # centre of the circle through S, M, E
    ax, ay, bx, by, cx, cy = sy, sz, my, mz, ey, ez
    d = 2 * (ax * (by - cy) + bx * (cy - ay) + cx * (ay - by))
    ux = ((ax * ax + ay * ay) * (by - cy) + (bx * bx + by * by) * (cy - ay)
          + (cx * cx + cy * cy) * (ay - by)) / d
    uy = ((ax * ax + ay * ay) * (cx - bx) + (bx * bx + by * by) * (ax - cx)
          + (cx * cx + cy * cy) * (bx - ax)) / d

    def rad(p):
        vx, vy = p[0] - ux, p[1] - uy
        n = math.hypot(vx, vy)
        return vx / n, vy / n

    def off(p, r):
        rx, ry = rad(p)
        return (p[0] + rx * r, p[1] + ry * r)

    h = UA_HALF_W
    S, M, E = (sy, sz), (my, mz), (ey, ez)
    rsx, rsy = rad(S)
    rex, rey = rad(E)
    ts = (rsy, -rsx) if (rsy * dy - rsx * dz) < 0 else (-rsy, rsx)
    te = (-rey, rex) if (-rey * dy + rex * dz) > 0 else (rey, -rex)
    far_s = (sy + ts[0] * h, sz + ts[1] * h)
    far_e = (ey + te[0] * h, ez + te[1] * h)
    prof = (cq.Workplane("YZ").workplane(offset=UA_X0)
            .moveTo(*off(S, h)).threePointArc(off(M, h), off(E, h))
            .threePointArc(far_e, off(E, -h))
            .threePointArc(off(M, -h), off(S, -h))
            .threePointArc(far_s, off(S, h)).close())
    link = prof.extrude(UA_X1 - UA_X0)
    link = safe_fillet(link, "not |X", UA_FILLET)
    # hub bosses (rims) on the +X side, recessed faces with screw holes
    xf = UA_X1
    for (py, pz), r in (((sy, sz), SHOULDER_HUB_R), ((ey, ez), ELBOW_HUB_R)):
        boss = xcyl(r, xf - UA_FILLET - 1.0, xf + 0.8, py, pz)
        boss = safe_fillet(boss, ">X", 1.2)
        link = link.union(boss)
        link = link.cut(xcyl(r - 3.0, xf - 1.2, xf + 1, py, pz))
        link = link.cut(xcyl(2.2, xf - 8, xf + 1, py, pz))
        for dz_ in (6.5, -6.5):
            link = link.cut(xcyl(0.9, xf - 8, xf + 1, py, pz + dz_))
    return link


upper = upper_link().rotate((0, SHOULDER[0], SHOULDER[1]),
                             (0, ELBOW[0], ELBOW[1]), UA_TWIST)

# =========================== FOREARM (arm frame) ===========================
FT = tilt_of(ELBOW, WRIST)
FL = math.hypot(WRIST[0] - ELBOW[0], WRIST[1] - ELBOW[1])
fxc = 0.5 * (FA_X0 + FA_X1)
fth = FA_X1 - FA_X0

# elbow section: block behind the upper-arm hub, rounded about the elbow axis
ep = (cq.Workplane("YZ").workplane(offset=FA_BACK)
      .moveTo(FORE_OFF - FORE_W / 2, 34.5).lineTo(FORE_OFF - FORE_W / 2, 0)
      .threePointArc((FORE_OFF, -FORE_W / 2), (FORE_OFF + FORE_W / 2, 0))
      .lineTo(FORE_OFF + FORE_W / 2, 34.5).close()
      .extrude(FA_X1 - FA_BACK))
ep = safe_fillet(ep, "|X", 1.5)
# roll sleeve (middle section): large rounding on the outer edge
fore_mid = lbox(fth - 1.0, FORE_W - 1.5, 40, fxc - 0.5, FORE_OFF, 56.0)
try:
    fore_mid = fore_mid.edges("|Z").edges(">X").edges("<Y").fillet(9.0)
except Exception:
    pass
fore_mid = safe_fillet(fore_mid, "|Z and <X", 2.0)
# wrist section
fore_up = lbox(fth, FORE_W, 45, fxc, FORE_OFF, 99.0)
fore_up = safe_fillet(fore_up, "|Z", 3.0)
# core joining the sections (leaves narrow grooves between them)
web = lbox(fth - 5, FORE_W - 5, 90, fxc, FORE_OFF, 60)
fore = ep.union(fore_mid).union(fore_up).union(web)
# window on the front face of the sleeve with the roll shaft inside
win_x = FA_X0 + 10.0
fore = fore.cut(lbox(11, 12, 38, win_x, FORE_OFF - FORE_W / 2, 56.0))
fore = fore.union(lbox(5, 8, 40, win_x, FORE_OFF - FORE_W / 2 + 6, 56.0))
# wrist plate on +X side with oval slot
WP_T = 5.0                     # wrist plate thickness
wy0, wy1 = FORE_OFF - FORE_W / 2 - 0.5, FORE_OFF + FORE_W / 2 + 0.5
wpr = (wy1 - wy0) / 2
wp = (cq.Workplane("YZ").workplane(offset=FA_X1 - 0.5)
      .moveTo(wy0, 82).lineTo(wy1, 82)
      .lineTo(wy1, FL + 8)
      .threePointArc((FORE_OFF, FL + 8 + wpr), (wy0, FL + 8))
      .close().extrude(WP_T + 0.5))
wp = safe_fillet(wp, "|X", 3.0)
wp = safe_fillet(wp, ">X", 1.2)
fore = fore.union(wp)
fore = fore.cut(cq.Workplane("YZ").workplane(offset=FA_X1 + 2)
                .center(0, FL).slot2D(11, 6, 90).extrude(6))
fore = place(fore, FT, ELBOW)
# elbow axle through the side plate into the upper-arm hub
fore = fore.union(xcyl(8.0, FA_BACK + 1.0, UA_X0 + 3.0, ELBOW[0], ELBOW[1]))

# elbow servo box (on -X side)
el_servo = lbox(24, 22, 36, FA_BACK - 12, 7, 6)
el_servo = safe_fillet(el_servo, "|X", 1.0)
el_servo = place(el_servo, FT, ELBOW)
# wrist servo box (on -X side)
wr_servo = lbox(21, 24, 32, FA_X0 - 10.5, FORE_OFF, FL + 5)
wr_servo = safe_fillet(wr_servo, "|X", 1.0)
wr_servo = place(wr_servo, FT, ELBOW)

# =========================== GRIPPER (arm frame) ===========================


def xz_slab(sketch, yc, th):
    """Extrude an XZ sketch symmetrically about local y = yc."""
    return sketch.extrude(th).translate((0, yc + th / 2, 0))


def bar(p0, p1, w, yc, th):
    """Rounded link bar between two points of the XZ plane."""
    ang = math.degrees(math.atan2(p1[0] - p0[0], p1[1] - p0[1]))
    ln = math.hypot(p1[0] - p0[0], p1[1] - p0[1])
    b = xz_slab(cq.Workplane("XZ").slot2D(ln + w, w, 90), yc, th)
    return b.rotate((0, 0, 0), (0, 1, 0), ang).translate(
        (0.5 * (p0[0] + p1[0]), 0, 0.5 * (p0[1] + p1[1])))


def gripper():
    g = lbox(30, 16, 16, 0, 0, 27)                      # gripper base
    g = safe_fillet(g, "|Y", 2.0)
    g = g.union(lbox(14, 14, 12, 0, 0, 16))             # wrist coupling
    g = g.union(lbox(44, 4, 26, 0, 6, 46))              # back plate
    g = g.union(lbox(10, 14, 26, 0, -1, 46))            # centre spine
    # gripper servo sticking out toward +Y
    g = g.union(safe_fillet(lbox(16, 22, 16, 0, 18, 40), "|X", 1.5))
    for sx in (-1, 1):
        gc = (sx * GEAR_DX, GEAR_Z)
        p1 = (sx * 28.0, 65.0)
        # gear disc with its lever arm (front layer) + back lever
        g = g.union(xz_slab(cq.Workplane("XZ").center(*gc).circle(GEAR_R),
                            GEAR_Y, 4.0))
        g = g.union(bar(gc, p1, 9.0, GEAR_Y, 4.0))
        g = g.union(bar(gc, p1, 9.0, 9.0, 2.5))
        # spur teeth on the gear (plain blocks)
        for k in range(-4, 5):
            a = -sx * 90.0 + 14.0 * k
            t = lbox(2.0, 4, 2.6, 0, GEAR_Y, GEAR_R + 0.8)
            t = t.rotate((0, 0, 0), (0, 1, 0), a).translate(
                (gc[0], 0, gc[1]))
            g = g.union(t)
        # idler links (front and back layers)
        a0, a1 = (sx * 4.7, 56.6), (sx * 19.5, 82.5)
        for yy in (-8.5, 8.5):
            g = g.union(bar(a0, a1, 7.0, yy, 2.5))
        # pivot pins
        for pp in (gc, p1, a0, a1):
            g = g.union(xz_slab(cq.Workplane("XZ").center(*pp).circle(1.8),
                                0.0, 24.0))
        # jaw (thick claw), built for the left side and mirrored
        jaw = (cq.Workplane("XZ")
               .moveTo(-32.0, 58.0)
               .threePointArc((-28.5, 87.0), (-17.0, 110.0))
               .threePointArc((-12.5, 111.0), (-8.5, 108.5))
               .threePointArc((-14.5, 90.0), (-18.5, 72.0))
               .lineTo(-21.0, 58.0)
               .close())
        jaw = safe_fillet(xz_slab(jaw, 0.0, JAW_T), "not |Y", 1.5)
        if sx > 0:
            jaw = jaw.mirror("YZ")
        g = g.union(jaw)
    return g


grip = place(gripper(), GRIP_TILT, WRIST, GX)

# =========================== ASSEMBLY ======================================
arm = (shoulder.union(upper).union(fore).union(el_servo).union(wr_servo)
       .union(grip))
arm = arm.rotate((0, 0, 0), (0, 0, 1), -ARM_YAW)

# small clip on top of the turntable (front)
clip = lbox(11, 5, 8, 0, -24, CAP_TOP + 4)
clip = safe_fillet(clip, "|Y", 1.0)
clip = clip.cut(lbox(5, 8, 4, 0, -24, CAP_TOP + 4.5))

result = base.union(clip).union(arm)

VIEW = {"azimuth": 45, "elevation": 26}
